import math
import cadquery as cq

# Round bowl / dish: spherical shell wall of uniform thickness, flat foot on the
# underside, a rolled (rounded) rim on the outside and a sharp inner rim edge under
# which the cavity wall is slightly undercut before blending into the spherical floor.
# The whole part is one revolved profile (sketched in the XZ plane, revolved about Z).

# ---------------- driving dimensions (mm) ----------------
R_MAX = 30.0        # max outer radius (equator of the rolled rim)
H = 15.3            # overall height (top of the rim)
R_FOOT = 10.0       # radius of the flat foot on the underside
RHO = 2.6           # radius of the rolled rim (outer side)
T_WALL = 2.4        # wall thickness of the spherical shell
R_EDGE = 25.3       # radius of the sharp inner rim edge
Z_EDGE = 14.65      # height of the sharp inner rim edge
F_UC = 3.4          # radius of the undercut fillet below the inner rim edge

VIEW = {"azimuth": 45, "elevation": 26}

RC = R_MAX - RHO    # rim bead centre radius
ZB = H - RHO        # rim bead centre height


def bisect(fn, lo, hi, n=200):
    flo = fn(lo)
    for _ in range(n):
        mid = 0.5 * (lo + hi)
        fm = fn(mid)
        if flo * fm <= 0:
            hi = mid
        else:
            lo, flo = mid, fm
    return 0.5 * (lo + hi)


def on_circle(cx, cz, r, ang):
    return (cx + r * math.cos(ang), cz + r * math.sin(ang))


def ang_of(cx, cz, p):
    return math.atan2(p[1] - cz, p[0] - cx)


# ---- outer wall: sphere (centre on axis) through the foot edge, tangent to the rim bead
RS = bisect(lambda rs: math.hypot(RC, ZB - math.sqrt(rs * rs - R_FOOT ** 2)) - (rs - RHO),
            R_MAX * 0.9, R_MAX * 20.0)
ZC = math.sqrt(RS * RS - R_FOOT ** 2)           # sphere centre height
_d = math.hypot(RC, ZB - ZC)
T1 = (RC + RHO * RC / _d, ZB + RHO * (ZB - ZC) / _d)   # wall / bead tangency
TOP = (RC, H)

# ---- top of the rim: arc tangent to the bead top, sloping down to the sharp edge
_dx, _dz = RC - R_EDGE, H - Z_EDGE
RHO_I = (_dx * _dx + _dz * _dz) / (2 * _dz)
EDGE = (R_EDGE, Z_EDGE)

# ---- cavity floor: sphere concentric with the outer wall (uniform shell)
RB = RS - T_WALL
Z_FLOOR = ZC - RB                               # lowest point of the cavity

# ---- undercut fillet: circle of radius F_UC through EDGE, tangent (inside) to the floor sphere
_r0, _r1 = RB - F_UC, F_UC
_ex, _ez = EDGE[0], EDGE[1] - ZC
_dd = math.hypot(_ex, _ez)
_a = (_r0 * _r0 - _r1 * _r1 + _dd * _dd) / (2 * _dd)
_h = math.sqrt(max(_r0 * _r0 - _a * _a, 0.0))
_xm, _zm = _a * _ex / _dd, ZC + _a * _ez / _dd
_c1 = (_xm + _h * _ez / _dd, _zm - _h * _ex / _dd)
_c2 = (_xm - _h * _ez / _dd, _zm + _h * _ex / _dd)
XF, ZF = min((_c1, _c2), key=lambda p: p[1])     # fillet centre (below the edge)
_a_edge = ang_of(XF, ZF, EDGE)                   # edge sits above the fillet equator
_a_tan = math.atan2(ZF - ZC, XF)                 # direction of floor tangency
T2 = on_circle(XF, ZF, F_UC, _a_tan)

# mid points for the three-point arcs
M_OUT = on_circle(0.0, ZC, RS, 0.5 * (ang_of(0.0, ZC, (R_FOOT, 0.0)) + ang_of(0.0, ZC, T1)))
M_BEAD = on_circle(RC, ZB, RHO, 0.5 * (ang_of(RC, ZB, T1) + math.pi / 2))
M_RIM = on_circle(RC, H - RHO_I, RHO_I, 0.5 * (math.pi / 2 + ang_of(RC, H - RHO_I, EDGE)))
M_UC = on_circle(XF, ZF, F_UC, 0.5 * (_a_edge + _a_tan))
M_FLOOR = on_circle(0.0, ZC, RB, 0.5 * (ang_of(0.0, ZC, T2) - math.pi / 2))

profile = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R_FOOT, 0)                          # flat foot
    .threePointArc(M_OUT, T1)                   # spherical outer wall
    .threePointArc(M_BEAD, TOP)                 # rolled rim, outer half
    .threePointArc(M_RIM, EDGE)                 # rim top sloping to the sharp inner edge
    .threePointArc(M_UC, T2)                    # undercut fillet under the edge
    .threePointArc(M_FLOOR, (0.0, Z_FLOOR))     # spherical cavity floor
    .close()
)

# revolve about the Z axis; the (purely cosmetic) revolve seam is turned to face
# the side of the part so it lies on the silhouette in the default view
SEAM_ANGLE = 45.0
result = profile.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
